import cadquery as cq

# =====================================================================
# Hook / clamp bracket.
#   X : thickness (W)      Y : length (L), hook opens toward +Y
#   Z : height (H)
# A "G"-shaped side profile (YZ) is extruded through the thickness,
# every edge is rounded, then a pocket is cut under the -X side (leaving
# a thin +X wall), a rib hangs from the pocket ceiling, and the holes,
# keyhole slot and engraved logo are added.
# =====================================================================

# ---------------- overall size (mm) ----------------
W = 19.5          # thickness along X
L = 46.0          # length along Y
H = 60.0          # height along Z

# top-front (-Y, +Z) chamfer
CH_TOP_Z = 44.2   # chamfer start on the -Y face
CH_TOP_Y = 16.0   # chamfer end on the top face

# hook ("G") at the +Y end
ARM_BOT_Z = 53.4      # underside of the top arm
SLOT_Y0 = 30.0        # vertical slot, -Y wall
SLOT_Y1 = 35.65       # vertical slot, +Y wall
SLOT_BOT_Z = 24.9     # flat bottom of the vertical slot
BLOCK_TOP_Z = 44.1    # top of the lower (clamp) block

# bottom-back (+Y, -Z) 45 deg chamfer
BOT_FLAT_Y = 25.8     # end of the flat bottom
FOOT_Z = 18.2         # underside of the lower block at the +Y end

EDGE_R = 1.2          # general edge rounding

# ---------------- holes ----------------
HOLE_X = -0.85                          # hole axes sit slightly toward -X
BIG_Y = 24.4                            # vertical counterbored screw hole
BIG_D, BIG_CB_D, BIG_CB_DEPTH = 4.9, 8.8, 25.0
CB_CHAMFER = 0.4
SMALL_Y = 40.0                          # clamp screw through arm + block
SMALL_D_ARM, SMALL_D_BLOCK = 4.8, 2.8
SMALL_INS_DEPTH = 6.0                   # insert bore at top of the block
FRONT_Z, FRONT_D = 8.9, 4.6             # cross hole in the -Y face
KEY_D = 4.0                             # keyhole slot depth behind pocket wall

# ---------------- pocket under the -X side ----------------
WALL_T = 1.6          # remaining wall on the +X side
POCKET_Z = 19.0       # pocket ceiling
POCKET_Y0 = 6.8       # solid front block length
# rib hanging from the ceiling (X measured from the -X face)
RIB_X0, RIB_XB, RIB_X1 = 3.3, 6.5, 11.0   # -X face, bottom end, slope top
RIB_Y0 = 17.5         # rib runs from here to the +Y end
RIB_Z = 15.2          # rib lower edge

# ---------------- engraved logo on the -Y face ----------------
LOGO_W, LOGO_H = 12.1, 12.5
LOGO_CX, LOGO_CZ = 0.0, 27.7
LOGO_DEPTH = 0.4
# shield with a stylised "S": one closed outline, normalised to the logo box
LOGO_UV = [
    (0.000, 1.000), (1.000, 1.000), (1.000, 0.522), (0.848, 0.616),
    (0.848, 0.853), (0.366, 0.853), (1.000, 0.414), (1.000, 0.357),
    (0.499, 0.000), (0.000, 0.339), (0.000, 0.769), (0.427, 0.467),
    (0.123, 0.457), (0.512, 0.200), (0.755, 0.367), (0.000, 0.894),
]

x0 = -W / 2.0                 # the -X face
foot_y = BOT_FLAT_Y + FOOT_Z  # end of the 45 deg bottom chamfer

# ---------------- main G profile (YZ plane), extruded along X ----------------
prof = (
    cq.Workplane("YZ")
    .moveTo(0, 0)
    .lineTo(BOT_FLAT_Y, 0)
    .lineTo(foot_y, FOOT_Z)
    .lineTo(L, FOOT_Z)
    .lineTo(L, BLOCK_TOP_Z)
    .lineTo(SLOT_Y1, BLOCK_TOP_Z)
    .lineTo(SLOT_Y1, SLOT_BOT_Z)
    .lineTo(SLOT_Y0, SLOT_BOT_Z)
    .lineTo(SLOT_Y0, ARM_BOT_Z)
    .lineTo(L, ARM_BOT_Z)
    .lineTo(L, H)
    .lineTo(CH_TOP_Y, H)
    .lineTo(0, CH_TOP_Z)
    .close()
    .extrude(W)
    .translate((x0, 0, 0))
)
body = prof.edges().fillet(EDGE_R)

# ---------------- pocket open to -X and to the bottom ----------------
pocket = (
    cq.Workplane("XY")
    .box(W - WALL_T + 5.0, L - POCKET_Y0 + 5.0, POCKET_Z + 5.0, centered=False)
    .translate((x0 - 5.0, POCKET_Y0, -5.0))
)
body = body.cut(pocket)

# rib under the pocket ceiling: vertical -X face, sloped +X face
rib = (
    cq.Workplane("XZ")
    .polyline([
        (x0 + RIB_X0, POCKET_Z + 0.5),
        (x0 + RIB_X0, RIB_Z),
        (x0 + RIB_XB, RIB_Z),
        (x0 + RIB_X1, POCKET_Z - 0.3),
        (x0 + RIB_X1, POCKET_Z + 0.5),
    ]).close()
    .extrude(-(L - RIB_Y0))          # XZ normal is -Y, so this runs toward +Y
    .translate((0, RIB_Y0, 0))
)
body = body.union(rib)

# ---------------- holes ----------------
# vertical counterbored hole from the top, through into the pocket
cbore = (
    cq.Workplane("XY").workplane(offset=H)
    .center(HOLE_X, BIG_Y).circle(BIG_CB_D / 2.0).extrude(-BIG_CB_DEPTH)
)
cb_chamfer = cq.Solid.makeCone(
    BIG_CB_D / 2.0 - 0.1, BIG_CB_D / 2.0 + CB_CHAMFER + 0.5, CB_CHAMFER + 0.6,
    pnt=cq.Vector(HOLE_X, BIG_Y, H - CB_CHAMFER - 0.1), dir=cq.Vector(0, 0, 1),
)
big_thru = cq.Workplane("XY").center(HOLE_X, BIG_Y).circle(BIG_D / 2.0).extrude(H)
body = body.cut(cbore).cut(cq.Workplane("XY").add(cb_chamfer)).cut(big_thru)

# clamp screw: clearance in the arm, insert bore + pilot hole in the block
small_arm = (
    cq.Workplane("XY").workplane(offset=ARM_BOT_Z - 1)
    .center(HOLE_X, SMALL_Y).circle(SMALL_D_ARM / 2.0).extrude(H)
)
small_ins = (
    cq.Workplane("XY").workplane(offset=BLOCK_TOP_Z + 1)
    .center(HOLE_X, SMALL_Y).circle(SMALL_D_ARM / 2.0).extrude(-(SMALL_INS_DEPTH + 1))
)
small_thru = cq.Workplane("XY").center(HOLE_X, SMALL_Y).circle(SMALL_D_BLOCK / 2.0).extrude(H)
body = body.cut(small_arm).cut(small_ins).cut(small_thru)

# cross hole along Y through the front block into the pocket
front = (
    cq.Workplane("XZ").workplane(offset=1)
    .center(HOLE_X, FRONT_Z).circle(FRONT_D / 2.0).extrude(-(POCKET_Y0 + 2))
)
body = body.cut(front)

# keyhole slot joining the cross hole to the -X face, open to the pocket;
# its back wall rounds out tangentially into the -X face (pin lead-in)
key_prism = (
    cq.Workplane("XZ").workplane(offset=-(POCKET_Y0 - KEY_D - 1.0))
    .center((x0 - 1 + HOLE_X) / 2.0, FRONT_Z)
    .slot2D(HOLE_X - (x0 - 1) + FRONT_D, FRONT_D)
    .extrude(-(KEY_D + 3.0))
)
key_plan = (
    cq.Workplane("XY").workplane(offset=FRONT_Z - 4)
    .moveTo(x0 - 1.0, POCKET_Y0 + 2.0)
    .lineTo(x0, POCKET_Y0 + 2.0)
    .lineTo(x0, POCKET_Y0)
    .radiusArc((x0 + KEY_D, POCKET_Y0 - KEY_D), -KEY_D)
    .lineTo(HOLE_X + 4.0, POCKET_Y0 - KEY_D)
    .lineTo(HOLE_X + 4.0, POCKET_Y0 + 2.0)
    .close()
    .extrude(8)
)
body = body.cut(key_prism.intersect(key_plan))

# ---------------- logo engraved into the -Y face ----------------
logo_pts = [
    (LOGO_CX + (u - 0.5) * LOGO_W, LOGO_CZ + (v - 0.5) * LOGO_H) for u, v in LOGO_UV
]
logo = (
    cq.Workplane("XZ").workplane(offset=LOGO_DEPTH)   # plane at Y = -depth
    .polyline(logo_pts).close()
    .extrude(-2.0 * LOGO_DEPTH)                       # to Y = +depth
)
body = body.cut(logo)

result = body
